import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.7            # back plate width  (X)
H = 120.0           # back plate height (Z)
T_BACK = 2.25       # back plate thickness (+Y side)
T_FRONT = 2.15      # front (raised) layer thickness (-Y side)
STEP = 2.1          # inset of the front layer from the back plate edge
R_CORNER = 3.0      # corner radius of the back plate

NOTCH_W = 22.9      # bottom notch width
NOTCH_D = 17.0      # bottom notch depth

HEX_W = 4.55        # hexagon across flats (horizontal, pointy-top hexes)
PITCH_X = 6.8       # hex pitch along a row
PITCH_Z = 5.66      # row pitch
N_ROWS = 20
N_COLS = 11         # hexes in the long rows (short rows have N_COLS-1)
HEX_DX = -0.4       # small sideways offset of the whole hex grid
EDGE_MARGIN = 0.8   # min web between hex and front-layer edge
NOTCH_MARGIN = 1.5  # min web between hex and notch

SLOT_X = 22.6       # slot centre offset from the vertical centre line
SLOT_Z = 14.65      # slot centre height above plate centre
SLOT_L = 25.0       # slot overall length
SLOT_W = 1.9        # slot width
SLOT_FLARE = 0.45   # outer slot wall drafted: front opening this much wider
SLOT_PAD = 1.8      # solid web left around each slot

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
WF = W - 2 * STEP
HF = H - 2 * STEP
R_HEX = HEX_W / math.sqrt(3.0)          # circumradius of the hexagon
T_ALL = T_BACK + T_FRONT

# ---------------- base plates ----------------
back = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(-T_BACK)                    # XZ normal is -Y -> goes to +Y
    .edges("|Y")
    .fillet(R_CORNER)
)
front = cq.Workplane("XZ").rect(WF, HF).extrude(T_FRONT)   # goes to -Y
plate = back.union(front)

# ---------------- bottom notch ----------------
notch = (
    cq.Workplane("XY")
    .box(NOTCH_W, T_ALL + 2.0, NOTCH_D + 1.0)
    .translate((0, (T_BACK - T_FRONT) / 2.0, -H / 2 + (NOTCH_D - 1.0) / 2.0))
)
plate = plate.cut(notch)

# ---------------- hexagon pattern ----------------
hex_pts = [
    (R_HEX * math.cos(math.radians(90 + 60 * i)),
     R_HEX * math.sin(math.radians(90 + 60 * i)))
    for i in range(6)
]
hex_proto = (
    cq.Workplane("XZ", origin=(0, T_BACK + 0.5, 0))
    .polyline(hex_pts)
    .close()
    .extrude(T_ALL + 1.0)
    .val()
)

x_lim = WF / 2 - EDGE_MARGIN - HEX_W / 2
z_lim = HF / 2 - EDGE_MARGIN - R_HEX
notch_x = NOTCH_W / 2 + NOTCH_MARGIN + HEX_W / 2
notch_z = -H / 2 + NOTCH_D + NOTCH_MARGIN + R_HEX

centres = []
for r in range(N_ROWS):
    z = (N_ROWS - 1) / 2.0 * PITCH_Z - r * PITCH_Z
    n = N_COLS if r % 2 == 0 else N_COLS - 1
    for c in range(n):
        x = (c - (n - 1) / 2.0) * PITCH_X + HEX_DX
        if abs(x) > x_lim + 1e-6 or abs(z) > z_lim + 1e-6:
            continue
        if abs(x) < notch_x and z < notch_z:
            continue
        centres.append((x, z))

hexes = [hex_proto.translate(cq.Vector(x, 0, z)) for (x, z) in centres]
plate = plate.cut(cq.Workplane("XY").newObject([cq.Compound.makeCompound(hexes)]))

# ---------------- slots with solid web around them ----------------
for sx in (-SLOT_X, SLOT_X):
    pad = (
        cq.Workplane("XZ", origin=(sx, T_BACK, SLOT_Z))
        .slot2D(SLOT_L + 2 * SLOT_PAD, SLOT_W + 2 * SLOT_PAD, angle=90)
        .extrude(T_ALL)
    )
    plate = plate.union(pad)


def slot_section(sx, y):
    """Slot outline at depth y: the inner wall is straight, the outer wall
    flares so the slot is SLOT_FLARE wider on the front face than on the back."""
    side = 1.0 if sx > 0 else -1.0
    x_in = sx - side * SLOT_W / 2.0
    flare = SLOT_FLARE * (T_BACK - y) / T_ALL
    x_out = sx + side * (SLOT_W / 2.0 + flare)
    return (
        cq.Workplane("XZ", origin=((x_in + x_out) / 2.0, y, SLOT_Z))
        .slot2D(SLOT_L, abs(x_out - x_in), angle=90)
        .wires()
        .val()
    )


for sx in (-SLOT_X, SLOT_X):
    tool = cq.Solid.makeLoft(
        [slot_section(sx, T_BACK + 0.5), slot_section(sx, -T_FRONT - 0.5)], True
    )
    plate = plate.cut(cq.Workplane("XY").newObject([tool]))

result = plate.clean()
